import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 200.0      # length along Y
H = 50.7       # height along Z
T = 18.0       # thickness along X (front face at X=T, back face at X=0)

# main front recess
REC_Y = 88.0           # recess half length
REC_Z0 = 4.3           # recess bottom
REC_Z1 = 46.9          # recess top
FLOOR_X = 4.0          # recess floor level (depth = T - FLOOR_X)

# bottom ledge inside the recess
LEDGE_Z1 = 13.2
LEDGE_X = 9.5

# narrow shelves at the recess ends
SHELF_X = 7.3
SHELF_W_NEG = 3.2
SHELF_W_POS = 1.7

# keyhole (spring tab) pockets
PF = 2.2               # pocket floor level
KP_Z0, KP_Z1 = 14.5, 42.2
KP_W = 16.0
KP_YC = [-26.75, -5.5, 23.4, 55.65]
HEAD_Z = 34.3
TAB_A = 3.8            # tongue half width
SLIT_W = 1.6
HEAD_R = 5.5
LEG_END_Z = 15.5
TONGUE_X = 1.6         # front surface of the thinned tongue strip
TONGUE_TIP_X = 0.6     # front surface of the (thinner) tongue head
HEAD_STEP = 6.3        # step between strip and head, below the head centre
DISC_R = 4.2           # button top radius (base radius = head radius)
DISC_TOP_X = 5.7

# -Y end horizontal tab pocket
HP_Y0, HP_Y1 = -79.0, -50.9
HP_Z0, HP_Z1 = 26.9, 42.5
HT_YC, HT_ZC = -58.7, 34.5
HT_R = 5.2             # head radius
HT_W = 1.8             # slit width
HT_TZ0, HT_TZ1 = 30.5, HT_ZC + HT_R   # tongue lower / upper edge
HT_LEG_END_Y = -77.0
HT_DISC_R = 4.2
HT_DISC_TOP_X = 5.5

# block with small hole under it
BLK_Y0, BLK_Y1 = -70.0, -48.7
BLK_Z0, BLK_Z1 = LEDGE_Z1, HP_Z0
BLK_H = 0.5
BLK_HOLE = (-62.9, 21.9, 5.0, 8.5)   # y, z, d, back countersink d

# +Y end through hole
END_HOLE = (71.4, 23.2, 8.4, 12.5)

# corner mounting holes
MH_Y = 92.7
MH_Z = (7.5, 38.2)
MH_D = 6.0
MH_CSK = 10.5


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def xcyl(x0, x1, y, z, r):
    return (cq.Workplane("YZ", origin=(x0, y, z))
            .circle(r).extrude(x1 - x0))


def csk_hole(y, z, d, dk):
    """through hole along X with a 90 deg countersink on the back face (X=0)"""
    h = (dk - d) / 2.0
    cone = cq.Solid.makeCone(dk / 2.0 + 0.5, d / 2.0, h + 0.5,
                             pnt=cq.Vector(-0.5, y, z), dir=cq.Vector(1, 0, 0))
    return xcyl(-1, T + 1, y, z, d / 2).union(cq.Workplane().add(cone))


def button(x0, x1, y, z, r0, r1):
    """tapered round push button along +X: radius r0 at X=x0, r1 at X=x1"""
    cone = cq.Solid.makeCone(r0, r1, x1 - x0, pnt=cq.Vector(x0, y, z), dir=cq.Vector(1, 0, 0))
    return cq.Workplane().add(cone)


# ---------------- base body ----------------
body = box(0, T, -L / 2, L / 2, 0, H)

# main recess
body = body.cut(box(FLOOR_X, T + 1, -REC_Y, REC_Y, REC_Z0, REC_Z1))

# ledge along the bottom of the recess
body = body.union(box(FLOOR_X - 0.01, LEDGE_X, -REC_Y, REC_Y, REC_Z0 - 0.01, LEDGE_Z1))

# narrow raised shelves along both end walls of the recess
body = body.union(box(FLOOR_X - 0.01, SHELF_X, -REC_Y, -REC_Y + SHELF_W_NEG, LEDGE_Z1 - 0.01, REC_Z1 + 0.01))
body = body.union(box(FLOOR_X - 0.01, SHELF_X, REC_Y - SHELF_W_POS, REC_Y, LEDGE_Z1 - 0.01, REC_Z1 + 0.01))

# ---------------- vertical keyhole spring tabs ----------------
for yc in KP_YC:
    body = body.cut(box(PF, FLOOR_X + 0.01, yc - KP_W / 2, yc + KP_W / 2, KP_Z0, KP_Z1))
    ro = HEAD_R + SLIT_W
    # tongue outline (head + strip)
    inner = (xcyl(-2, PF + 1, yc, HEAD_Z, HEAD_R)
             .union(box(-2, PF + 1, yc - TAB_A, yc + TAB_A, LEG_END_Z - 6, HEAD_Z)))
    # thinned tongue strip and even thinner head
    top_z = HEAD_Z + HEAD_R + 1
    body = body.cut(box(TONGUE_X, PF + 0.5, yc - ro, yc + ro, LEG_END_Z, top_z).intersect(inner))
    body = body.cut(box(TONGUE_TIP_X, PF + 0.5, yc - ro, yc + ro, HEAD_Z - HEAD_STEP, top_z)
                    .intersect(inner))
    # U-shaped through slit around the tongue
    outer = (xcyl(-1, PF + 0.01, yc, HEAD_Z, ro)
             .union(box(-1, PF + 0.01, yc - TAB_A - SLIT_W, yc + TAB_A + SLIT_W, LEG_END_Z, HEAD_Z))
             .union(xcyl(-1, PF + 0.01, yc - TAB_A - SLIT_W / 2, LEG_END_Z, SLIT_W / 2))
             .union(xcyl(-1, PF + 0.01, yc + TAB_A + SLIT_W / 2, LEG_END_Z, SLIT_W / 2)))
    body = body.cut(outer.cut(inner))
    # round push button on the tongue head
    body = body.union(button(TONGUE_TIP_X, DISC_TOP_X, yc, HEAD_Z, HEAD_R - 0.05, DISC_R))

# ---------------- -Y end horizontal tab ----------------
body = body.cut(box(PF, FLOOR_X + 0.01, HP_Y0, HP_Y1, HP_Z0, HP_Z1))
ro = HT_R + HT_W
inner = (xcyl(-2, PF + 1, HT_YC, HT_ZC, HT_R)
         .union(box(-2, PF + 1, HT_LEG_END_Y - 6, HT_YC, HT_TZ0, HT_TZ1)))
tip_y = HT_YC + HT_R + 1
body = body.cut(box(TONGUE_X, PF + 0.5, HT_LEG_END_Y, tip_y, HT_ZC - ro, HT_ZC + ro).intersect(inner))
body = body.cut(box(TONGUE_TIP_X, PF + 0.5, HT_YC - HEAD_STEP, tip_y, HT_ZC - ro, HT_ZC + ro)
                .intersect(inner))
outer = (xcyl(-1, PF + 0.01, HT_YC, HT_ZC, ro)
         .union(box(-1, PF + 0.01, HT_LEG_END_Y, HT_YC, HT_TZ0 - HT_W, HT_TZ1 + HT_W))
         .union(xcyl(-1, PF + 0.01, HT_LEG_END_Y, HT_TZ0 - HT_W / 2, HT_W / 2))
         .union(xcyl(-1, PF + 0.01, HT_LEG_END_Y, HT_TZ1 + HT_W / 2, HT_W / 2)))
body = body.cut(outer.cut(inner))
body = body.union(button(TONGUE_TIP_X, HT_DISC_TOP_X, HT_YC, HT_ZC, HT_R - 0.05, HT_DISC_R))

# block pad with a through hole
body = body.union(box(FLOOR_X - 0.01, FLOOR_X + BLK_H, BLK_Y0, BLK_Y1, BLK_Z0 - 0.01, BLK_Z1))
body = body.cut(csk_hole(*BLK_HOLE))

# +Y end through hole
body = body.cut(csk_hole(*END_HOLE))

# corner mounting holes
for sy in (-1, 1):
    for mz in MH_Z:
        body = body.cut(csk_hole(sy * MH_Y, mz, MH_D, MH_CSK))

result = body
